import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 240.0          # overall length along Y (measured on the +X side)
W = 25.0           # overall width along X
H = 63.5           # overall height (posts)
P = 29.2           # post length along Y (on the +X side)
T_BAR = 15.0       # connecting bar thickness
BAR_Z0 = 15.5      # bar bottom height (= foot thickness)
FOOT = 68.0        # foot length from the outer end (includes the post)
END_ANGLE = 8.5    # plan-view slant of the end faces (deg), ends longer on +X
R_END = 6.5        # vertical round where each end face meets the -X side
HOLE_D = 6.5       # through hole in each post
CB_D = 18.5        # counterbore diameter (from the bottom)
CB_DEPTH = 20.0    # counterbore depth

VIEW = {"azimuth": 45, "elevation": 26}

hy = L / 2.0
d = W * math.tan(math.radians(END_ANGLE))   # end slant offset across the width

# ---------------- plan outline (XY) ----------------
# trapezoid: +X side is the full length, the ends slant inwards toward -X;
# the two -X vertical corners are rounded.
plan = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .polyline([
        (W / 2.0, -hy),
        (W / 2.0, hy),
        (-W / 2.0, hy - d),
        (-W / 2.0, -hy + d),
    ])
    .close()
    .extrude(H + 2.0)
    .edges("|Z").edges("<X")
    .fillet(R_END)
)


# ---------------- end blocks: post + foot (L-profile in YZ) ----------------
def end_block(sign):
    y_out = sign * (hy + 1.0)
    y_post = sign * (hy - P)
    y_foot = sign * (hy - FOOT)
    prof = [
        (y_out, 0.0),
        (y_foot, 0.0),
        (y_foot, BAR_Z0),
        (y_post, BAR_Z0),
        (y_post, H),
        (y_out, H),
    ]
    blk = (
        cq.Workplane("YZ", origin=(-W / 2.0 - 1.0, 0, 0))
        .polyline(prof).close()
        .extrude(W + 2.0)
        .intersect(plan)
    )
    # through hole from the top, large counterbore from the bottom
    yc = sign * (hy - P / 2.0)
    thru = (cq.Workplane("XY", origin=(0, yc, -1.0))
            .circle(HOLE_D / 2.0).extrude(H + 2.0))
    cbore = (cq.Workplane("XY", origin=(0, yc, -1.0))
             .circle(CB_D / 2.0).extrude(CB_DEPTH + 1.0))
    return blk.cut(thru).cut(cbore)


left = end_block(-1.0)
right = end_block(1.0)

# ---------------- connecting bar: spans between the posts, sits on the feet --
bar = (
    cq.Workplane("XY", origin=(0, 0, BAR_Z0))
    .rect(W, L - 2.0 * P)
    .extrude(T_BAR)
)

# The part is three bodies in contact (two L-shaped end blocks and the bar),
# as in the original model.
result = cq.Workplane("XY").newObject([left.val(), bar.val(), right.val()])
